import math
import cadquery as cq

# variable-radius fillet builder (re-exported by cadquery's kernel module)
BRepFilletAPI_MakeFillet = cq.occ_impl.shapes.BRepFilletAPI_MakeFillet

# ---------------------------------------------------------------
# Robot-joint style housing.
# Z up, top flange face at Z = 0; the lower motor axis runs along Y,
# its stepped output face looks toward -Y (front).
# ---------------------------------------------------------------

# --- top flange (axis Z) ---
R_LIP = 50.0          # top lip radius
H_LIP = 9.8           # lip height
TOP_CHAMFER = 2.0
R_BAND = 48.9         # main band radius
Z_BAND_BOT = -29.3    # bottom of the band
R_LOWER = 45.1        # lower ring radius
Z_LOWER_BOT = -39.7   # bottom of the flange
LOWER_FILLET = 2.0
FLAT_K = 0.95         # slope dX/dZ of the side chamfer on the band
FLAT_Z0 = -22.6       # height where that chamfer meets the band surface
LOWER_X_TOP = 40.9    # half width (X) of the elliptical lower ring at its top
LOWER_X_BOT = 37.2    # ... and at its bottom
ARCH_W = 12.3         # arch notch (front/back of band)
ARCH_TOP = -19.5
ARCH_DEPTH = 1.5
GROOVE_Z = -10.7      # short marking grooves under the lip
GROOVE_SPAN = 26.0

# --- body: keyhole profile (XZ) extruded along Y ---
NECK_W = 36.5         # half width of the neck column
ZC = -132.5           # motor axis height
R_H = 48.3            # motor housing radius
TAPER = 0.25          # neck flare slope dX/dZ toward the housing
KINK_R = 45.0         # blend radius between neck and flare
Z_COL_TOP = -36.0     # top of the body column (under the flange)
Y_FRONT = 2.0         # front face of the housing / column
Y_SEAM = 39.0         # seam between housing and rear cover
SEAM_GAP = 0.8
SEAM_DEPTH = 0.7
REAR_INSET = 0.6

# rear cover dome: side profile revolved about a vertical axis at Y = Y_AX
Y_AX = -13.9
REAR_PTS = [(44.0, -33.0), (50.0, -34.2), (53.5, -39.0), (57.5, -65.0), (61.3, -110.0),
            (62.6, -135.0), (59.5, -158.0), (51.0, -174.0), (39.0, -181.0)]
BOSS_Y = 47.2        # centre of the round end of the D bosses
BOSS_ZS = (-41.0, -90.0, -133.0, -168.0)
BOSS_H = 8.6
BOSS_FLAT = 4.0
BOSS_OUT = 0.6

# --- chin under the flange (in front of the column) ---
Y_CHIN = -29.6        # front face of the chin
Z_CHIN_BOT = -71.4    # lowest point of the chin
CHIN_R = 16.0         # bottom rounding of the chin cup (side view)
CHIN_CUP_R = 33.0     # plan radius of the chin cup
CHIN_V_R = 11.0       # bottom radius of the V outline (front view)
CHIN_BLEND = 12.0     # blend between the cup and the V flanks

# --- motor face stack (along -Y) ---
R_RING = 45.4         # ring behind the lugs
Y_RING = -7.0         # front face of that ring
Y_LUG = -11.7         # front of the lugs
LUG_W = 6.0
LUG_FRONT_R = 1.8
N_LUGS = 12
STRIP_DEPTH = 0.5     # shallow strip on the disc where the lugs sit
FRONT_EDGE_R = 2.5    # rounding of the housing front edge
COL_EDGE_R = 10.0     # rounding of the neck front corners
R_DISC = 38.9
LUG_SINK = 0.3       # lugs reach this far into the disc
Y_DISC = -21.4
R_STEP = 30.5
Y_STEP = -23.4
R_FLANGE = 19.8
Y_FLANGE = -27.2
R_BOSS = 13.8
Y_BOSS = -31.0
BOSS_CONE = 2.2

# --- small details ---
TAB_Y = (14.0, 38.0)
TAB_H = 10.0
TAB_OUT = 1.4


# ================================================================
def zcyl(r, z0, z1, seam_deg=45.0):
    s = cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
    return s.rotate((0, 0, 0), (0, 0, 1), seam_deg)


def ycyl(r, y0, y1):
    """Cylinder on the motor axis from y0 to y1 (y0 < y1), seam at the top."""
    s = (cq.Workplane("XZ").workplane(offset=-y1)
         .circle(r).extrude(y1 - y0))
    return s.rotate((0, 0, 0), (0, 1, 0), -90).translate((0, 0, ZC))


def keyhole_pts(inset=0.0):
    w = NECK_W - inset
    r = R_H - inset
    ln = math.hypot(1.0, TAPER)
    tx, tz = r / ln, ZC + r * TAPER / ln          # flare tangent on circle
    z_k = tz + (tx - w) / TAPER                  # kink height on the neck side
    d2 = ((tx - w) / math.hypot(tx - w, tz - z_k), (tz - z_k) / math.hypot(tx - w, tz - z_k))
    th = math.atan(TAPER)
    t = KINK_R * math.tan(th / 2)
    t1 = (w, z_k + t)
    t2 = (w + d2[0] * t, z_k + d2[1] * t)
    return w, r, (tx, tz), t1, t2


def xz_keyhole(inset=0.0, z_top=Z_COL_TOP):
    w, r, (tx, tz), t1, t2 = keyhole_pts(inset)
    wp = (cq.Workplane("XZ")
          .moveTo(-w, z_top)
          .lineTo(w, z_top)
          .lineTo(*t1)
          .tangentArcPoint(t2, relative=False)
          .lineTo(tx, tz)
          .threePointArc((0, ZC - r), (-tx, tz))
          .lineTo(-t2[0], t2[1])
          .tangentArcPoint((-t1[0], t1[1]), relative=False)
          .close())
    return wp


def body_column(y0, y1, inset=0.0, z_top=Z_COL_TOP):
    # XZ workplane normal is -Y: extrude negative to go toward +Y
    return xz_keyhole(inset, z_top).extrude(-(y1 - y0)).translate((0, y0, 0))


def var_front_fillet(solid_wp, r_col, r_ring, z_top):
    """Round the front outline of the body: large radius on the neck corners,
    small radius around the motor housing, linear blend along the flare."""
    sol = solid_wp.val()
    face = solid_wp.faces("<Y").val()
    mk = BRepFilletAPI_MakeFillet(sol.wrapped)
    for e in face.Edges():
        p0, p1 = e.startPoint(), e.endPoint()
        if abs(p0.z - z_top) < 1e-6 and abs(p1.z - z_top) < 1e-6:
            continue                                   # top edge stays sharp
        gt = e.geomType()
        if gt == "CIRCLE" and abs(p0.z - p1.z) < 1e-6:
            mk.Add(r_ring, e.wrapped)                  # housing arc
        elif gt == "LINE" and abs(p0.x - p1.x) > 1e-6:
            ra, rb = (r_col, r_ring) if p0.z > p1.z else (r_ring, r_col)
            mk.Add(ra, rb, e.wrapped)                  # flare line
        else:
            mk.Add(r_col, e.wrapped)                   # neck sides and kink arcs
    mk.Build()
    return cq.Workplane().add(cq.Shape.cast(mk.Shape()))


def half_width_at(z, inset=0.0):
    """Half width of the keyhole outline at height z."""
    w, r, (tx, tz), t1, t2 = keyhole_pts(inset)
    if z >= t1[1]:
        return w
    if z <= tz:
        return math.sqrt(max(r * r - (z - ZC) ** 2, 0.0))
    return tx - (z - tz) * TAPER


# ================= top flange =================
lip = zcyl(R_LIP, -H_LIP, 0.0).faces(">Z").edges().chamfer(TOP_CHAMFER)
band = zcyl(R_BAND, Z_BAND_BOT, -H_LIP + 0.01)
# lower ring: elliptical, narrower across X and tapering toward the neck
lower = (cq.Workplane("XY").workplane(offset=Z_LOWER_BOT)
         .ellipse(R_LOWER - 0.6, LOWER_X_BOT)
         .workplane(offset=Z_BAND_BOT + 0.01 - Z_LOWER_BOT)
         .ellipse(R_LOWER, LOWER_X_TOP)
         .loft(ruled=True)
         .faces("<Z").edges().fillet(LOWER_FILLET)
         .rotate((0, 0, 0), (0, 0, 1), 90))
flange = lip.union(band).union(lower)

# inclined side flats at +/-X under the flange
def flat_cutters(sgn):
    x_bb = R_BAND - FLAT_K * (FLAT_Z0 - Z_BAND_BOT)
    c1 = (cq.Workplane("XZ")
          .polyline([(sgn * R_BAND, FLAT_Z0), (sgn * (R_BAND + 20), FLAT_Z0),
                     (sgn * (R_BAND + 20), Z_BAND_BOT), (sgn * x_bb, Z_BAND_BOT)])
          .close().extrude(-60, both=True))
    return c1


for sgn in (1, -1):
    flange = flange.cut(flat_cutters(sgn))

# arch shaped notches on the band (front and back)
arch_r = ARCH_W / 2
arch = (cq.Workplane("XZ")
        .center(0, ARCH_TOP - arch_r).circle(arch_r)
        .extrude(-6).translate((0, -R_BAND - 1.0, 0))
        .union(cq.Workplane("XY")
               .box(ARCH_W, 6, (ARCH_TOP - arch_r) - (Z_BAND_BOT - 1))
               .translate((0, -R_BAND + 2.0, ((ARCH_TOP - arch_r) + (Z_BAND_BOT - 1)) / 2))))
arch = arch.intersect(zcyl(R_BAND + 2, Z_BAND_BOT - 2, 0).cut(zcyl(R_BAND - ARCH_DEPTH, -60, 5)))
for a in (0, 180):
    flange = flange.cut(arch.rotate((0, 0, 0), (0, 0, 1), a))

# short marking grooves just under the lip
g_ring = zcyl(R_BAND + 1, GROOVE_Z - 0.45, GROOVE_Z + 0.45).cut(zcyl(R_BAND - 0.5, -40, 5))
g_box = cq.Workplane("XY").box(GROOVE_SPAN, 20, 4).translate((0, -R_BAND, GROOVE_Z))
g_seg = g_ring.intersect(g_box)
for a in (0, 90, 180, 270):
    flange = flange.cut(g_seg.rotate((0, 0, 0), (0, 0, 1), a))

# ================= body =================
front_housing = var_front_fillet(body_column(Y_FRONT, Y_SEAM), COL_EDGE_R, FRONT_EDGE_R, Z_COL_TOP)

# rear cover: keyhole prism intersected with a revolved dome
prof = cq.Workplane("YZ", origin=(0, Y_AX, 0))   # local x -> +Y, local y -> +Z
rp = [(y - Y_AX, z) for (y, z) in REAR_PTS]
dome = (prof.moveTo(0, rp[0][1])
        .lineTo(rp[0][0], rp[0][1])
        .spline(rp[1:], includeCurrent=True)
        .lineTo(0, rp[-1][1] - 10)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
rear_prism = body_column(Y_SEAM + SEAM_GAP, Y_SEAM + 40, inset=REAR_INSET, z_top=-33.0)
rear = rear_prism.intersect(dome)
seam_core = body_column(Y_SEAM - 0.01, Y_SEAM + SEAM_GAP + 0.01, inset=SEAM_DEPTH,
                        z_top=Z_COL_TOP - SEAM_DEPTH)

body = front_housing.union(rear).union(seam_core)

# D shaped screw bosses along the rear cover sides
def d_boss():
    h = BOSS_H / 2
    return (cq.Workplane("YZ")
            .moveTo(-BOSS_FLAT, -h).lineTo(0, -h)
            .threePointArc((h, 0), (0, h))
            .lineTo(-BOSS_FLAT, h).close()
            .extrude(BOSS_OUT + 3.0)
            .faces(">X").edges().fillet(0.6)
            .translate((-3.0, 0, 0)))


for s in (1, -1):
    for bz in BOSS_ZS:
        x0 = half_width_at(bz, REAR_INSET)
        b = d_boss()
        if bz < ZC - 20:
            # on the round lower part the boss follows the radial direction
            ang = math.degrees(math.atan2(bz - ZC, x0))
            b = b.rotate((0, 0, 0), (0, 1, 0), -ang)
        b = b.translate((x0, BOSS_Y, bz))
        if s < 0:
            b = b.mirror("YZ")
        body = body.union(b)

# chin under the flange: a round-bottomed cup carved by a V shaped prism
cup = (cq.Workplane("YZ", origin=(0, Y_CHIN + CHIN_CUP_R, 0))
       .moveTo(0, Z_COL_TOP)
       .lineTo(CHIN_CUP_R, Z_COL_TOP)
       .lineTo(CHIN_CUP_R, Z_CHIN_BOT + CHIN_R)
       .radiusArc((CHIN_CUP_R - CHIN_R, Z_CHIN_BOT), CHIN_R)
       .lineTo(0, Z_CHIN_BOT)
       .close()
       .revolve(360, (0, 0, 0), (0, 1, 0)))
# V outline (front view) with a rounded bottom
vc = (0.0, Z_CHIN_BOT + CHIN_V_R)
p0 = (NECK_W, Z_LOWER_BOT - 0.8)
dx, dz = p0[0] - vc[0], p0[1] - vc[1]
dd = math.hypot(dx, dz)
ang = math.atan2(dz, dx) - math.acos(CHIN_V_R / dd)
tp = (vc[0] + CHIN_V_R * math.cos(ang), vc[1] + CHIN_V_R * math.sin(ang))
vprism = (cq.Workplane("XZ")
          .moveTo(-NECK_W, Z_COL_TOP)
          .lineTo(NECK_W, Z_COL_TOP)
          .lineTo(*p0)
          .lineTo(*tp)
          .threePointArc((0, Z_CHIN_BOT), (-tp[0], tp[1]))
          .lineTo(-p0[0], p0[1])
          .close()
          .extrude(-(Y_FRONT + 0.5 - Y_CHIN + 1)).translate((0, Y_CHIN - 1, 0)))
chin = cup.intersect(vprism)
chin = chin.edges(cq.selectors.BoxSelector((-40, Y_CHIN - 10, Z_CHIN_BOT - 9),
                                           (40, Y_FRONT - 2.5, Z_COL_TOP - 1))).fillet(CHIN_BLEND)
body = body.union(chin)

# small rectangular pad on the -X side of the housing
tab = (cq.Workplane("XY")
       .box(TAB_OUT + 4, TAB_Y[1] - TAB_Y[0], TAB_H)
       .edges("|X").fillet(2.0)
       .translate((-(R_H + TAB_OUT) + (TAB_OUT + 4) / 2, (TAB_Y[0] + TAB_Y[1]) / 2, ZC)))
body = body.union(tab)

# small flat spot on the underside
body = body.cut(cq.Workplane("XY").box(14, 11, 4).translate((0, 23.5, ZC - R_H - 2 + 0.7)))

# ================= motor face stack =================
ring = ycyl(R_RING, Y_RING, Y_FRONT + 0.5)
lug0 = (cq.Workplane("XY")
        .box(LUG_W, Y_RING - Y_LUG + 0.5, R_RING - R_DISC + LUG_SINK)
        .edges("|Y and <Z").fillet(LUG_W / 2 - 0.3)
        .faces("<Y").edges(">Z").fillet(LUG_FRONT_R)
        .translate((0, (Y_LUG + Y_RING + 0.5) / 2, (R_RING + R_DISC - LUG_SINK) / 2)))
lugs = [lug0.rotate((0, 0, 0), (0, 1, 0), i * 360.0 / N_LUGS).translate((0, 0, ZC)).val()
        for i in range(N_LUGS)]
ring = ring.union(cq.Workplane().add(cq.Compound.makeCompound(lugs)))

disc = (ycyl(R_DISC, Y_DISC, Y_LUG).faces("<Y").edges().chamfer(0.8)
        .union(ycyl(R_DISC - STRIP_DEPTH, Y_LUG - 0.01, Y_RING + 0.5)))
step = ycyl(R_STEP, Y_STEP, Y_DISC + 0.5)
fl = ycyl(R_FLANGE, Y_FLANGE, Y_STEP + 0.5).faces("<Y").edges().chamfer(0.6)
boss = ycyl(R_BOSS, Y_BOSS, Y_FLANGE + 0.5)
cone = (cq.Workplane().add(cq.Solid.makeCone(R_BOSS - 1.2, 0.8, BOSS_CONE,
                                              cq.Vector(0, Y_BOSS + 0.01, 0), cq.Vector(0, -1, 0)))
        .translate((0, 0, ZC)))
face_stack = ring.union(disc).union(step).union(fl).union(boss).union(cone)

result = flange.union(body).union(face_stack)
